import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.gp import gp_Pnt

# =====================================================================
# Rotary bearing bracket (C-frame with two bearing arms) + back clamp
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 77.0                 # overall width in X (arms, back wall, back plate)
R = W / 2.0              # radius of the rounded arm fronts (arc centre at X=Y=0)
Y_BACK = 47.5            # body back face
WALL_T = 6.1             # back wall thickness (Y)
GAP_H = 25.63            # half height of the opening between the arms
BODY_H = 46.0            # half height of the body (outer faces of the arms)
CAP_T = 3.85             # cover disc thickness
CAP_R = R - 0.35         # cover disc radius
CAP_HOLE_R = 33.9        # cover screw pitch radius (holes at 45 deg)
CAP_HOLE_D = 3.9
CAP_HOLE_DEPTH = 8.0

# bearing seats + bearings (one in each arm, facing the opening)
SEAT_D = 59.9
SEAT_DEPTH = 12.0
RELIEF_D = 26.7            # shaft bore behind the bearing (same as inner ring bore)
BRG_RECESS = 0.45        # bearing face sits this far below the arm face
OR_ID = 48.3             # outer ring bore
IR_OD = 37.2             # inner ring outside diameter
IR_ID = 26.7             # inner ring bore
BALL_D = 7.4
N_BALLS = 10

# back wall, front face (facing the opening)
HOLE_X = 20.4            # 4 screw holes, one of them counterbored
HOLE_Z = 11.45
HOLE_D = 6.8
CB_D = 14.0
CB_DEPTH = 2.0
E_X, E_Z, E_D = 10.15, 19.05, 4.0          # small hole near the top
POCKET_X0 = 24.1                        # rounded pocket open to the +X side
POCKET_H = 12.4
POCKET_DEPTH = 2.4
POCKET_R = 2.0
F_X, F_D, F_CSK = 28.5, 3.4, 5.3         # countersunk hole in the pocket

# side holes in the upper arm
SIDE_Y = Y_BACK - 7.55
SIDE_Z1, SIDE_Z2 = 42.05, 34.4           # two small countersunk holes on +X
SIDE_D, SIDE_CSK = 2.8, 4.0
BIG_SIDE_D = 12.3                        # large blind hole on -X
BIG_SIDE_Z = 36.0
BIG_SIDE_DEPTH = 10.0

# small vertical hole in the lower arm near the back wall
LOW_HOLE_Y = 33.4
LOW_HOLE_D = 6.2
LOW_HOLE_DEPTH = 10.0

# back clamp piece (extruded profile along X)
BP_T = 13.1              # back plate thickness (Y)
RAIL_D = 10.45           # rail protrusion behind the back plate (Y)
BP_ZC = 0.625            # back piece centre height
BP_HALF = 46.625         # back piece half height
RAIL_HALF = 16.68        # rail half height
NECK_HALF = 6.53         # slot opening towards the body
TOOTH_T = 4.3
CAV_WIDE_HALF = 16.38    # undercut part of the slot
CAV_NARROW_HALF = 13.59  # slot inside the rail
CAV_WIDE_END = Y_BACK + 9.45
CAV_TRANS_END = Y_BACK + 14.25
RAIL_WALL = 3.85
RAIL_FIL_OUT = 2.5
RAIL_FIL_IN = 2.1
BP_HOLE_X = 10.2
BP_HOLE_Z = (41.9, 22.9)  # measured from the back piece centre
BP_HOLE_D = 3.0
BP_HOLE_DEPTH = 10.0
RAIL_HOLE_X = 19.0
RAIL_HOLE_D = 3.5

S2 = math.sqrt(2.0) / 2.0


# ---------------- helpers ----------------
def nurbs_chain(segs, to3d):
    """One exact rational quadratic B-spline edge through a G1 chain of
    line / circular-arc segments.
    segs: ('L', p0, p1) or ('A', p0, corner, p1, weight) in 2D."""
    poles, wts = [], []
    for i, s in enumerate(segs):
        if s[0] == "L":
            p0, p1 = s[1], s[2]
            mid = ((p0[0] + p1[0]) / 2.0, (p0[1] + p1[1]) / 2.0)
            seg_p, seg_w = [p0, mid, p1], [1.0, 1.0, 1.0]
        else:
            seg_p, seg_w = [s[1], s[2], s[3]], [1.0, s[4], 1.0]
        if i == 0:
            poles += seg_p
            wts += seg_w
        else:
            poles += seg_p[1:]
            wts += seg_w[1:]
    n = len(segs)
    P = TColgp_Array1OfPnt(1, len(poles))
    Wt = TColStd_Array1OfReal(1, len(poles))
    for i, (p, w) in enumerate(zip(poles, wts)):
        P.SetValue(i + 1, gp_Pnt(*to3d(p)))
        Wt.SetValue(i + 1, w)
    K = TColStd_Array1OfReal(1, n + 1)
    M = TColStd_Array1OfInteger(1, n + 1)
    for i in range(n + 1):
        K.SetValue(i + 1, float(i))
        M.SetValue(i + 1, 3 if i in (0, n) else 2)
    crv = Geom_BSplineCurve(P, Wt, K, M, 2)
    return cq.Edge(BRepBuilderAPI_MakeEdge(crv).Edge())


def line3(p0, p1, to3d):
    return cq.Edge.makeLine(cq.Vector(*to3d(p0)), cq.Vector(*to3d(p1)))


def prism(edges, vec):
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Workplane("XY").newObject([cq.Solid.extrudeLinear(face, cq.Vector(*vec))])


def zcyl(r, z0, h, seam=(1, 0, 0), c=(0, 0)):
    """Cylinder along +Z; 'seam' sets where the cylinder seam line lies."""
    pl = cq.Plane(origin=(c[0], c[1], z0), xDir=seam, normal=(0, 0, 1))
    return cq.Workplane(pl).circle(r).extrude(h)


def axis_hole(origin, direction, d, depth, seam, csk=None):
    """Drill solid: cylinder from 'origin' along 'direction', optional 90 deg countersink."""
    pl = cq.Plane(origin=origin, xDir=seam, normal=direction)
    tool = cq.Workplane(pl).circle(d / 2.0).extrude(depth)
    if csk:
        h = (csk - d) / 2.0
        cone = cq.Solid.makeCone(
            csk / 2.0 + 0.2, d / 2.0, h + 0.2,
            pnt=cq.Vector(*origin) - cq.Vector(*direction) * 0.2,
            dir=cq.Vector(*direction),
        )
        tool = tool.union(cq.Workplane("XY").newObject([cone]))
    return tool


# ---------------- body ----------------
def d_outline_prism(z0, z1):
    to3d = lambda p: (p[0], p[1], z0)
    u = nurbs_chain(
        [
            ("L", (-R, Y_BACK), (-R, 0.0)),
            ("A", (-R, 0.0), (-R, -R), (0.0, -R), S2),
            ("A", (0.0, -R), (R, -R), (R, 0.0), S2),
            ("L", (R, 0.0), (R, Y_BACK)),
        ],
        to3d,
    )
    back = line3((R, Y_BACK), (-R, Y_BACK), to3d)
    return prism([u, back], (0, 0, z1 - z0))


# one full-height extrusion of the D outline, then the opening is cut
body = d_outline_prism(-BODY_H, BODY_H)
gap = (
    cq.Workplane("XY")
    .box(W + 2.0, Y_BACK - WALL_T + R + 1.0, 2 * GAP_H, centered=(True, False, True))
    .translate((0, -R - 1.0, 0))
)
body = body.cut(gap)

# cover discs (seams placed at the back)
body = body.union(zcyl(CAP_R, BODY_H, CAP_T, seam=(0, 1, 0)))
body = body.union(zcyl(CAP_R, -BODY_H - CAP_T, CAP_T, seam=(0, 1, 0)))

# cover screw holes
for a in (45, 135, 225, 315):
    hx = CAP_HOLE_R * math.cos(math.radians(a))
    hy = CAP_HOLE_R * math.sin(math.radians(a))
    body = body.cut(zcyl(CAP_HOLE_D / 2, BODY_H + CAP_T - CAP_HOLE_DEPTH, CAP_HOLE_DEPTH + 0.01, c=(hx, hy)))
    body = body.cut(zcyl(CAP_HOLE_D / 2, -BODY_H - CAP_T - 0.01, CAP_HOLE_DEPTH, c=(hx, hy)))

# bearing seats (from the opening side) + relief bores behind them
relief_h = BODY_H - GAP_H - SEAT_DEPTH
body = body.cut(zcyl(SEAT_D / 2, GAP_H, SEAT_DEPTH))
body = body.cut(zcyl(RELIEF_D / 2, GAP_H + SEAT_DEPTH - 0.01, relief_h + 0.01))
body = body.cut(zcyl(SEAT_D / 2, -GAP_H - SEAT_DEPTH, SEAT_DEPTH))
body = body.cut(zcyl(RELIEF_D / 2, -BODY_H, relief_h + 0.01))

# ball bearings pressed into the seats
BRG_W = SEAT_DEPTH - BRG_RECESS


def bearing(z0):
    outer = zcyl(SEAT_D / 2, z0, BRG_W, seam=(0, 1, 0)).cut(zcyl(OR_ID / 2, z0 - 0.01, BRG_W + 0.02))
    inner = zcyl(IR_OD / 2, z0, BRG_W, seam=(0, 1, 0)).cut(zcyl(IR_ID / 2, z0 - 0.01, BRG_W + 0.02))
    brg = outer.union(inner)
    pitch = (OR_ID + IR_OD) / 4.0
    zc = z0 + BRG_W / 2.0
    for i in range(N_BALLS):
        a = 2 * math.pi * (i + 0.5) / N_BALLS
        ball = cq.Workplane("XY").newObject(
            [cq.Solid.makeSphere(BALL_D / 2, cq.Vector(pitch * math.cos(a), pitch * math.sin(a), zc))]
        )
        brg = brg.union(ball)
    return brg


body = body.union(bearing(GAP_H + BRG_RECESS))
body = body.union(bearing(-GAP_H - BRG_RECESS - BRG_W))

# back wall front face features
Y_WF = Y_BACK - WALL_T          # front face of the back wall
into_wall = (0, 1, 0)
for (hx, hz) in ((-HOLE_X, HOLE_Z), (-HOLE_X, -HOLE_Z), (HOLE_X, -HOLE_Z), (HOLE_X, HOLE_Z)):
    body = body.cut(axis_hole((hx, Y_WF - 0.01, hz), into_wall, HOLE_D, WALL_T + 0.02, (1, 0, 0)))
body = body.cut(axis_hole((HOLE_X, Y_WF - 0.01, HOLE_Z), into_wall, CB_D, CB_DEPTH + 0.01, (1, 0, 0)))
body = body.cut(axis_hole((E_X, Y_WF - 0.01, E_Z), into_wall, E_D, WALL_T + 0.02, (1, 0, 0)))

# rounded pocket, open towards +X (rounded corners on the closed side)
pk_w = R - POCKET_X0 + 1.0
pocket = (
    cq.Workplane("XZ", origin=(0, Y_WF + POCKET_DEPTH, 0))
    .center(POCKET_X0 + pk_w / 2.0, 0)
    .rect(pk_w, POCKET_H)
    .extrude(POCKET_DEPTH + 0.01)
    .edges("|Y and <X")
    .fillet(POCKET_R)
)
body = body.cut(pocket)
body = body.cut(
    axis_hole((F_X, Y_WF + POCKET_DEPTH - 0.01, 0), into_wall, F_D, WALL_T, (1, 0, 0), csk=F_CSK)
)

# side holes in the upper arm
for z in (SIDE_Z1, SIDE_Z2):
    body = body.cut(axis_hole((R + 0.01, SIDE_Y, z), (-1, 0, 0), SIDE_D, 10.0, (0, 0, 1), csk=SIDE_CSK))
body = body.cut(axis_hole((-R - 0.01, SIDE_Y, BIG_SIDE_Z), (1, 0, 0), BIG_SIDE_D, BIG_SIDE_DEPTH, (0, 0, 1)))

# vertical hole in the lower arm top face
body = body.cut(zcyl(LOW_HOLE_D / 2, -GAP_H - LOW_HOLE_DEPTH, LOW_HOLE_DEPTH + 0.01, c=(0, LOW_HOLE_Y)))

# ---------------- back clamp piece ----------------
y0 = Y_BACK
y_bp = Y_BACK + BP_T
y_rail = y_bp + RAIL_D
y_tooth = y0 + TOOTH_T
y_cav_end = y_rail - RAIL_WALL
fo, fi = RAIL_FIL_OUT, RAIL_FIL_IN

# S-shaped step of the slot ceiling: two tangent arcs of equal radius
dy_s = CAV_TRANS_END - CAV_WIDE_END
dz_s = CAV_WIDE_HALF - CAV_NARROW_HALF
half_turn = math.atan2(dz_s, dy_s)
r_s = (dy_s / 2.0) / (2.0 * math.sin(half_turn) * math.cos(half_turn))  # dy/(2 sin(theta))
ym, zm = CAV_WIDE_END + dy_s / 2.0, CAV_WIDE_HALF - dz_s / 2.0


def arc_mid(p0, p1, centre):
    """Mid point of the minor circular arc p0->p1 about 'centre'."""
    a0 = math.atan2(p0[1] - centre[1], p0[0] - centre[0])
    a1 = math.atan2(p1[1] - centre[1], p1[0] - centre[0])
    da = (a1 - a0 + math.pi) % (2 * math.pi) - math.pi
    am = a0 + da / 2.0
    rr = math.hypot(p0[0] - centre[0], p0[1] - centre[1])
    return (centre[0] + rr * math.cos(am), centre[1] + rr * math.sin(am))


def fillet_mid(corner, d0, d1, r):
    """Mid point of a 90 deg fillet of radius r in a corner; d0/d1 unit vectors
    from the corner along the two legs."""
    c = (corner[0] + (d0[0] + d1[0]) * r, corner[1] + (d0[1] + d1[1]) * r)
    k = r / math.sqrt(2.0)
    return (c[0] - (d0[0] + d1[0]) * k, c[1] - (d0[1] + d1[1]) * k)


sp = cq.Workplane("YZ")
sp = sp.moveTo(y0, -BP_HALF).lineTo(y_bp, -BP_HALF)
# lower concave fillet, rail, convex corners, upper concave fillet
sp = sp.lineTo(y_bp, -RAIL_HALF - fi)
sp = sp.threePointArc(fillet_mid((y_bp, -RAIL_HALF), (0, -1), (1, 0), fi), (y_bp + fi, -RAIL_HALF))
sp = sp.lineTo(y_rail - fo, -RAIL_HALF)
sp = sp.threePointArc(fillet_mid((y_rail, -RAIL_HALF), (-1, 0), (0, 1), fo), (y_rail, -RAIL_HALF + fo))
sp = sp.lineTo(y_rail, RAIL_HALF - fo)
sp = sp.threePointArc(fillet_mid((y_rail, RAIL_HALF), (0, -1), (-1, 0), fo), (y_rail - fo, RAIL_HALF))
sp = sp.lineTo(y_bp + fi, RAIL_HALF)
sp = sp.threePointArc(fillet_mid((y_bp, RAIL_HALF), (1, 0), (0, 1), fi), (y_bp, RAIL_HALF + fi))
sp = sp.lineTo(y_bp, BP_HALF).lineTo(y0, BP_HALF)
# T-slot: neck, undercut, S-step, slot inside the rail
sp = sp.lineTo(y0, NECK_HALF).lineTo(y_tooth, NECK_HALF).lineTo(y_tooth, CAV_WIDE_HALF)
sp = sp.lineTo(CAV_WIDE_END, CAV_WIDE_HALF)
cA = (CAV_WIDE_END, CAV_WIDE_HALF - r_s)
cB = (CAV_TRANS_END, CAV_NARROW_HALF + r_s)
sp = sp.threePointArc(arc_mid((CAV_WIDE_END, CAV_WIDE_HALF), (ym, zm), cA), (ym, zm))
sp = sp.threePointArc(arc_mid((ym, zm), (CAV_TRANS_END, CAV_NARROW_HALF), cB), (CAV_TRANS_END, CAV_NARROW_HALF))
sp = sp.lineTo(y_cav_end, CAV_NARROW_HALF).lineTo(y_cav_end, -CAV_NARROW_HALF)
sp = sp.lineTo(CAV_TRANS_END, -CAV_NARROW_HALF)
cB2 = (CAV_TRANS_END, -CAV_NARROW_HALF - r_s)
cA2 = (CAV_WIDE_END, -CAV_WIDE_HALF + r_s)
sp = sp.threePointArc(arc_mid((CAV_TRANS_END, -CAV_NARROW_HALF), (ym, -zm), cB2), (ym, -zm))
sp = sp.threePointArc(arc_mid((ym, -zm), (CAV_WIDE_END, -CAV_WIDE_HALF), cA2), (CAV_WIDE_END, -CAV_WIDE_HALF))
sp = sp.lineTo(y_tooth, -CAV_WIDE_HALF).lineTo(y_tooth, -NECK_HALF).lineTo(y0, -NECK_HALF)
sp = sp.close()
back = sp.extrude(W).translate((-W / 2.0, 0, BP_ZC))

# back plate screw holes (2 x 2 above and below the rail)
for zs in (1, -1):
    for hz in BP_HOLE_Z:
        for hx in (-BP_HOLE_X, BP_HOLE_X):
            back = back.cut(
                axis_hole((hx, y_bp + 0.01, BP_ZC + zs * hz), (0, -1, 0), BP_HOLE_D, BP_HOLE_DEPTH, (0, 0, 1))
            )
# rail holes (through the rail back wall into the slot)
for hx in (-RAIL_HOLE_X, RAIL_HOLE_X):
    back = back.cut(
        axis_hole((hx, y_rail + 0.01, BP_ZC), (0, -1, 0), RAIL_HOLE_D, RAIL_WALL + 0.5, (0, 0, 1))
    )

# two separate bodies: bracket and back clamp, touching along the body back face
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound([body.val(), back.val()])])

VIEW = {"azimuth": 45, "elevation": 26}
